import cadquery as cq

# ---------------- overall lid dimensions (mm) ----------------
W = 110.0          # length along X
D = 90.0           # depth along Y
H = 30.3           # overall height
TOP = 3.4          # top plate thickness
WALL_LIP = 1.5     # wall thickness of the lower lip (internal rabbet)
LIP_H = 5.8        # height of the thin lip at the open bottom
WALL = 3.2         # wall thickness above the lip

# ---------------- internal ribs hanging from the ceiling ----------------
RIB_H = 4.5                    # rib depth below the ceiling
R1_Y0, R1_Y1 = 13.0, 17.8      # cross bar along X (full inner width)
R2_X0, R2_X1 = -30.6, -24.4    # left rib along Y (cross bar -> back wall)
R3_X0, R3_X1 = 22.0, 28.0      # right rib along Y (cross bar -> back wall)

# ---------------- lettering ----------------
GAME_LETTERS = "GAME"
GAME_X = (-13.0, -5.0, 2.8, 10.6)   # letter centres along X
GAME_Y = 22.9                       # letter centre along Y
GAME_SIZE = 6.2                     # font size (cap height ~4.5)
GAME_SX = (1.0, 0.95, 1.0, 1.3)     # per-glyph horizontal stretch (target face is wider)
GH_TXT = "github.com/sergey12malyshev"
GH_SIZE = 4.7
GH_X = 1.6                          # bbox centre of the address
GH_Y = -37.4
GH_DEPTH = 0.8                      # engraving depth of the address
GH_SX, GH_SY = 0.985, 1.1           # stretch: target serif face is taller/narrower

ZC = H - TOP  # ceiling height (underside of the top plate)


def letter_at(ch, size, cx, cy, z0, height, font, kind, sx=1.0):
    """One glyph extruded from z0 upward, stretched by sx along X and its
    bounding box centred on (cx, cy)."""
    g = cq.Workplane("XY").text(ch, size, height, font=font, kind=kind,
                                halign="center", valign="center").val()
    if abs(sx - 1.0) > 1e-9:
        g = g.transformGeometry(cq.Matrix([[sx, 0, 0, 0], [0, 1, 0, 0], [0, 0, 1, 0]]))
    bb = g.BoundingBox()
    dx = cx - 0.5 * (bb.xmin + bb.xmax)
    dy = cy - 0.5 * (bb.ymin + bb.ymax)
    return cq.Workplane("XY").add(g.translate(cq.Vector(dx, dy, z0)))


# ---- outer shell: box, open at the bottom, with an internal rabbet lip ----
body = cq.Workplane("XY").box(W, D, H, centered=(True, True, False))
lip_cav = cq.Workplane("XY").box(W - 2 * WALL_LIP, D - 2 * WALL_LIP, LIP_H,
                                 centered=(True, True, False))
main_cav = (cq.Workplane("XY")
            .box(W - 2 * WALL, D - 2 * WALL, ZC - LIP_H + 0.001, centered=(True, True, False))
            .translate((0, 0, LIP_H - 0.001)))
lid = body.cut(lip_cav).cut(main_cav)

# ---- ribs under the top plate ----
yin = D / 2 - WALL
xin = W / 2 - WALL
r1 = (cq.Workplane("XY").box(2 * xin, R1_Y1 - R1_Y0, RIB_H, centered=(True, False, False))
      .translate((0, R1_Y0, ZC - RIB_H)))
r2 = (cq.Workplane("XY").box(R2_X1 - R2_X0, yin - R1_Y1, RIB_H, centered=False)
      .translate((R2_X0, R1_Y1, ZC - RIB_H)))
r3 = (cq.Workplane("XY").box(R3_X1 - R3_X0, yin - R1_Y1, RIB_H, centered=False)
      .translate((R3_X0, R1_Y1, ZC - RIB_H)))
lid = lid.union(r1).union(r2).union(r3)

# ---- "G A M E" cut right through the top plate ----
for ch, cx, sx in zip(GAME_LETTERS, GAME_X, GAME_SX):
    g = letter_at(ch, GAME_SIZE, cx, GAME_Y, ZC - 0.5, TOP + 1.0, "DejaVu Sans", "bold", sx)
    lid = lid.cut(g)

# ---- engraved github address near the front edge ----
gh = (cq.Workplane("XY")
      .text(GH_TXT, GH_SIZE, GH_DEPTH + 0.5, font="DejaVu Serif", kind="bold",
            halign="center", valign="center").val()
      .transformGeometry(cq.Matrix([[GH_SX, 0, 0, 0], [0, GH_SY, 0, 0], [0, 0, 1, 0]])))
gh_bb = gh.BoundingBox()
gh = gh.translate(cq.Vector(GH_X - 0.5 * (gh_bb.xmin + gh_bb.xmax),
                            GH_Y - 0.5 * (gh_bb.ymin + gh_bb.ymax),
                            H - GH_DEPTH))
lid = lid.cut(cq.Workplane("XY").add(gh))

result = lid
